import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 259.0          # overall length of the top plate (X)
W = 30.0           # overall width of the top plate (Y)
R_PLAN = 10.5      # plan corner radius of the top plate
T_FLANGE = 1.5     # vertical edge of the plate below the chamfer
CHAMF = 3.0        # 45 deg chamfer around the top edge

INSET = 3.0        # lower body side inset from plate edge
H_BODY = 3.0       # height of lower body below the plate
WALL = 1.5         # side wall thickness of the lower body ring

N_SLOTS = 65
SLOT_PITCH = 3.51
SLOT_W = 1.5
SLOT_LEN = 18.0
SLOT_DEPTH = 1.5
SLOT_X0 = -1.7     # slot field offset along X

N_CELLS = 8        # vaulted pockets under the slot field
CELL_PITCH = 28.2
CELL_LEN = 18.5
CELL_X0 = 5.0      # centre of the pocket row along X
VAULT_H = 2.5      # rise of the vault above the plate underside

HOLE_D = 4.4
HOLE_END = 9.0     # hole centre distance from plate end
HOLE_Y = 8.0       # +X end holes at +/- HOLE_Y

TAB_W = 9.0        # locating tab at the +X end
GUSSET_W = 10.0    # 45 deg gussets under the plate ends

CAV_X0 = -L / 2 + 13.0           # start of underside cavity (-X end)
CAV_R = 1.0
CAV_X1 = L / 2 - 13.0           # end of underside cavity (+X end)

Z_PLATE = H_BODY                 # underside of the plate
Z_TOP = H_BODY + T_FLANGE + CHAMF


def rrect(wp, lx, ly, r):
    return wp.sketch().rect(lx, ly).vertices().fillet(r).finalize()


# ---------------- top plate with smooth 45 deg chamfer ----------------
plate = rrect(cq.Workplane("XY").workplane(offset=Z_PLATE), L, W, R_PLAN).extrude(T_FLANGE)
cap = rrect(cq.Workplane("XY").workplane(offset=Z_PLATE + T_FLANGE), L, W, R_PLAN).extrude(CHAMF, taper=45)
part = plate.union(cap)

# ---------------- lower body: vertical walls, 45 deg gussets at the ends ----------------
LB = L - 2 * INSET
WB = W - 2 * INSET
R_BODY = R_PLAN - INSET
body = rrect(cq.Workplane("XY"), LB, WB, R_BODY).extrude(H_BODY)

# 45 deg gusset filling the corner between body end and plate underside
gusset = (
    cq.Workplane("XZ")
    .polyline([(LB / 2 - 1.0, 0.0), (LB / 2, 0.0), (L / 2, H_BODY), (LB / 2 - 1.0, H_BODY)])
    .close()
    .extrude(GUSSET_W / 2, both=True)
)
body = body.union(gusset).union(gusset.mirror("YZ"))

# locating tab at +X end, flush with the plate end
tab = cq.Workplane("XY").box(INSET + 1.0, TAB_W, H_BODY, centered=(False, True, False)).translate(
    (LB / 2 - 1.0, 0, 0)
)
body = body.union(tab)
# nothing below the plate may stick out past the plate outline
outline = rrect(cq.Workplane("XY"), L, W, R_PLAN).extrude(H_BODY)
body = body.intersect(outline)
part = part.union(body)

# ---------------- underside cavity ----------------
WC = WB - 2 * WALL
cav_len = CAV_X1 - CAV_X0
cavity = (
    rrect(cq.Workplane("XY").workplane(offset=-0.5), cav_len, WC, CAV_R)
    .extrude(H_BODY + 0.5)
    .translate(((CAV_X0 + CAV_X1) / 2, 0, 0))
)
part = part.cut(cavity)

# barrel-vaulted pockets into the plate underside (vault axis along Y)
r_v = ((CELL_LEN / 2) ** 2 + VAULT_H ** 2) / (2 * VAULT_H)
zc = Z_PLATE + VAULT_H - r_v
cells_x0 = CELL_X0 - (N_CELLS - 1) * CELL_PITCH / 2
for i in range(N_CELLS):
    xc = cells_x0 + i * CELL_PITCH
    cyl = (
        cq.Workplane("XZ")
        .workplane(offset=-WC / 2)
        .center(xc, zc)
        .circle(r_v)
        .extrude(WC)
    )
    lim = cq.Workplane("XY").box(CELL_LEN, WC, VAULT_H + 0.5, centered=(True, True, False)).translate(
        (xc, 0, Z_PLATE - 0.5)
    )
    part = part.cut(cyl.intersect(lim))

# ---------------- blind slots in the top face ----------------
slot_pts = [(SLOT_X0 - (N_SLOTS - 1) * SLOT_PITCH / 2 + i * SLOT_PITCH, 0) for i in range(N_SLOTS)]
slots = (
    cq.Workplane("XY")
    .workplane(offset=Z_TOP - SLOT_DEPTH)
    .pushPoints(slot_pts)
    .rect(SLOT_W, SLOT_LEN)
    .extrude(SLOT_DEPTH + 1)
)
part = part.cut(slots)

# ---------------- fixing holes ----------------
hole_pts = [(-L / 2 + HOLE_END, 0), (L / 2 - HOLE_END, HOLE_Y), (L / 2 - HOLE_END, -HOLE_Y)]
holes = (
    cq.Workplane("XY")
    .workplane(offset=-1)
    .pushPoints(hole_pts)
    .circle(HOLE_D / 2)
    .extrude(Z_TOP + 2)
)
part = part.cut(holes)


result = part
